import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
BASE_D = 80.0        # base disc diameter
BASE_H = 19.0        # base disc thickness
HOLE_D = 5.5         # mounting hole diameter
HOLE_PCD = 65.0      # mounting hole pitch-circle diameter
HOLE_N = 4           # number of mounting holes (on the X / Y axes)

THREAD_D = 30.0      # major diameter of threaded stud (M30)
THREAD_L = 100.0     # stud length above base
PITCH = 3.5          # thread pitch (M30 coarse)
THREAD_DEPTH = 1.9   # radial depth of thread
CREST_FLAT = 0.25    # width of flat on crest
ROOT_W = 0.86        # root width of thread tooth as fraction of pitch
TOP_CHAMFER = 1.6    # chamfer at the stud tip

SEAM_ANGLE = 45.0    # angular position of the base disc's cylindrical seam (cosmetic)

R_MAJ = THREAD_D / 2.0
R_MIN = R_MAJ - THREAD_DEPTH
Z_AXIS = ((0, 0, 0), (0, 0, 1))

# ---------------- base disc with holes ----------------
base = (
    cq.Workplane("XY").circle(BASE_D / 2.0).extrude(BASE_H)
    .rotate(*Z_AXIS, SEAM_ANGLE)
)
holes = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .polarArray(HOLE_PCD / 2.0, 0, 360, HOLE_N)
    .circle(HOLE_D / 2.0).extrude(BASE_H + 2.0)
)
base = base.cut(holes)

# ---------------- stud core ----------------
z0 = BASE_H
core = (
    cq.Workplane("XY").workplane(offset=z0 - 1.0)
    .circle(R_MIN).extrude(THREAD_L + 3.0)   # overshoots; trimmed by envelope
)


# ---------------- helical thread (ruled faces between helices) ----------------
def helical_thread(r_root, r_crest, pitch, height, z_start, hw_root, hw_crest):
    """Trapezoidal-profile helical rib built from four ruled helical faces."""
    def hx(r, dz):
        w = cq.Wire.makeHelix(pitch, height, r)
        return w.translate(cq.Vector(0, 0, z_start + dz)).Edges()[0]

    e1 = hx(r_root, -hw_root)
    e2 = hx(r_crest, -hw_crest)
    e3 = hx(r_crest, hw_crest)
    e4 = hx(r_root, hw_root)
    ring = [e1, e2, e3, e4]
    faces = [
        cq.Face.makeRuledSurface(a, b)
        for a, b in zip(ring, ring[1:] + ring[:1])
    ]
    for end in (False, True):
        pts = [e.endPoint() if end else e.startPoint() for e in ring]
        faces.append(cq.Face.makeFromWires(cq.Wire.makePolygon(pts, close=True)))
    solid = cq.Solid.makeSolid(cq.Shell.makeShell(faces))
    if solid.Volume() < 0:
        solid = cq.Solid(solid.wrapped.Reversed())
    return solid


thread_solid = helical_thread(
    r_root=R_MIN - 0.3,
    r_crest=R_MAJ,
    pitch=PITCH,
    height=THREAD_L + 2 * PITCH,
    z_start=z0 - PITCH,          # starts inside the base, runs out of it
    hw_root=ROOT_W * PITCH / 2.0,
    hw_crest=CREST_FLAT / 2.0,
)
thread = cq.Workplane("XY").add(thread_solid)

# envelope: major cylinder with chamfered tip, trims the thread at the top
env = (
    cq.Workplane("XZ")
    .polyline([
        (0, z0 - 0.5),
        (R_MAJ + 1.0, z0 - 0.5),
        (R_MAJ + 1.0, z0 + THREAD_L - TOP_CHAMFER - 1.0),
        (R_MAJ - TOP_CHAMFER, z0 + THREAD_L),
        (0, z0 + THREAD_L),
    ]).close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

stud = core.union(thread, clean=False).intersect(env, clean=False)


# ---------------- safety net: annular-groove thread if the helix boolean fails ----------------
def stud_ok(wp):
    sols = wp.solids().vals()
    if len(sols) != 1 or not sols[0].isValid():
        return False
    v = sols[0].Volume()
    return math.pi * R_MIN ** 2 * THREAD_L < v < math.pi * R_MAJ ** 2 * (THREAD_L + 0.5)


def ring_groove_stud():
    hw_r = PITCH / 2.0 - ROOT_W * PITCH / 2.0 * 0.87   # half width of groove at root
    hw_o = PITCH / 2.0 - CREST_FLAT / 2.0               # half width of groove at crest
    blank = env.intersect(
        cq.Workplane("XY").workplane(offset=z0 - 0.5).circle(R_MAJ).extrude(THREAD_L + 1.0)
    )
    n = int(THREAD_L / PITCH)
    grooves = None
    for i in range(n):
        zc = z0 + PITCH / 2.0 + i * PITCH
        g = (
            cq.Workplane("XZ")
            .polyline([(R_MIN, zc - hw_r), (R_MAJ + 0.1, zc - hw_o - 0.05),
                       (R_MAJ + 0.1, zc + hw_o + 0.05), (R_MIN, zc + hw_r)]).close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
        )
        grooves = g if grooves is None else grooves.union(g)
    return blank.cut(grooves)


if not stud_ok(stud):
    stud = ring_groove_stud()

result = base.union(stud, clean=False)
